import math
import cadquery as cq

V = cq.Vector

# ---------------- driving dimensions (mm) ----------------
A_F = 20.0        # flange apothem (half width across the flats, X)
R_F = 4.0         # flange corner radius (plan view)
A_BX = 17.9       # body half width across the +-X flats
A_BS = 18.15      # body apothem of the four slanted faces
R_BY = 5.5        # body corner radius at the +-Y points
R_BS = 4.0        # body corner radius at the four side corners
FL_CH = 0.75      # chamfer on the flange top edge

Z_LB = 6.0        # top of the lower (terminal) block / bottom of body
Z_BT = 24.9       # top of body / bottom of the flange chamfer
Z_FC = 26.85      # top of chamfer / bottom of flange plate
Z_TOP = 28.4      # top face

# lower block (cross shape)
LB_X = 13.1       # half width of central part
LB_Y = 14.07      # half depth of central part
LB_TX = 6.57      # half width of the tab extension
LB_TY = 17.7      # half depth incl. tab extension

# contact cavities (T shaped, through)
CAV_X = 11.03     # half width of the long slot
CAV_Y0 = 3.96     # inner edge (towards centre)
CAV_Y1 = 10.69    # outer edge of long slot
CAV_TX = 4.41     # half width of the key
CAV_TY = 15.66    # outer edge of key
CAV_CH = 1.0      # chamfer on cavity rim

# side windows (shallow arched recesses on the 4 slanted faces)
WIN_CX = 12.4     # |x| of the window centre line (on the slanted face)
WIN_W = 7.7       # width
WIN_Z0 = 7.75     # bottom
WIN_Z1 = 24.85    # top of arch (just under the flange chamfer)
WIN_D = 1.3       # depth

# engraved letters
LET_X = 15.85
LET_Y = 6.77
LET_HW = 1.5      # centreline half width
LET_HH = 3.69     # centreline half height
LET_W = 1.25      # stroke width
LET_D = 0.5       # depth

# contact retention slots ("ears") at the ends of each long slot
EAR_X0 = 7.55     # inner x of the ear slot (runs out to CAV_X)
EAR_D = 1.1       # depth of the ear into the wall
EAR_Z = 25.15     # top of the ear slots (they are open at the bottom)

# bottom centre hole
HOLE_D = 5.05
HOLE_CS = 7.15
HOLE_DEPTH = 8.0


# ---------------- helpers ----------------
def rhex_wire(a, r, z):
    """Rounded regular hexagon, flats at +-X, points at +-Y."""
    Rc = (a - r) / math.cos(math.radians(30))
    verts = [90 + 60 * i for i in range(6)]
    edges = []
    pts = []
    for th in verts:
        t = math.radians(th)
        c = V(Rc * math.cos(t), Rc * math.sin(t), z)
        p_in = c + V(r * math.cos(t - math.radians(30)), r * math.sin(t - math.radians(30)), 0)
        p_mid = c + V(r * math.cos(t), r * math.sin(t), 0)
        p_out = c + V(r * math.cos(t + math.radians(30)), r * math.sin(t + math.radians(30)), 0)
        pts.append((p_in, p_mid, p_out))
    for i in range(6):
        p_in, p_mid, p_out = pts[i]
        edges.append(cq.Edge.makeThreePointArc(p_in, p_mid, p_out))
        nxt = pts[(i + 1) % 6][0]
        edges.append(cq.Edge.makeLine(p_out, nxt))
    return cq.Wire.assembleEdges(edges)


def rpoly_wire(lines, radii, z):
    """Convex polygon given as supporting lines (normal angle deg, offset) in CCW
    order, each corner (between line i and i+1) rounded with radii[i]."""
    n = len(lines)
    nv = [V(math.cos(math.radians(t)), math.sin(math.radians(t)), 0) for t, _ in lines]
    arcs = []
    for i in range(n):
        j = (i + 1) % n
        a1, a2 = lines[i][1] - radii[i], lines[j][1] - radii[i]
        n1, n2 = nv[i], nv[j]
        det = n1.x * n2.y - n1.y * n2.x
        cx = (a1 * n2.y - a2 * n1.y) / det
        cy = (n1.x * a2 - n2.x * a1) / det
        c = V(cx, cy, z)
        mid = (n1 + n2).normalized()
        arcs.append((c + n1 * radii[i], c + mid * radii[i], c + n2 * radii[i]))
    edges = []
    for i in range(n):
        p0, pm, p1 = arcs[i]
        edges.append(cq.Edge.makeThreePointArc(p0, pm, p1))
        edges.append(cq.Edge.makeLine(p1, arcs[(i + 1) % n][0]))
    return cq.Wire.assembleEdges(edges)


def body_wire(z):
    lines = [(0, A_BX), (60, A_BS), (120, A_BS), (180, A_BX), (240, A_BS), (300, A_BS)]
    radii = [R_BS, R_BY, R_BS, R_BS, R_BY, R_BS]
    return rpoly_wire(lines, radii, z)


def prism(wire, h):
    f = cq.Face.makeFromWires(wire)
    return cq.Solid.extrudeLinear(f, V(0, 0, h))


# ---------------- main body ----------------
flange = prism(rhex_wire(A_F, R_F, Z_FC), Z_TOP - Z_FC)
flange = cq.Workplane().add(flange).faces(">Z").edges().chamfer(FL_CH).val()

transition = cq.Solid.makeLoft([body_wire(Z_BT), rhex_wire(A_F, R_F, Z_FC)], True)
body = prism(body_wire(Z_LB), Z_BT - Z_LB)

# lower block outline (one quadrant, then mirrored)
# cross shaped block, trimmed by the body's slanted faces (corner cuts flush with the body)
q = [(LB_X, 0), (LB_X, LB_Y), (LB_TX, LB_Y), (LB_TX, LB_TY), (0, LB_TY)]
outline = q + [(-x, y) for (x, y) in reversed(q)][1:]
outline = outline + [(x, -y) for (x, y) in reversed(outline)][1:-1]
lower = cq.Workplane("XY").polyline(outline).close().extrude(Z_LB).val()
lower = lower.intersect(prism(body_wire(-1.0), Z_LB + 2.0))

part = cq.Workplane().add(body).union(transition).union(flange).union(lower)

# ---------------- contact cavities ----------------
def cavity_sketch(sign):
    pts = [(-CAV_X, CAV_Y0), (CAV_X, CAV_Y0), (CAV_X, CAV_Y1), (CAV_TX, CAV_Y1),
           (CAV_TX, CAV_TY), (-CAV_TX, CAV_TY), (-CAV_TX, CAV_Y1), (-CAV_X, CAV_Y1)]
    return [(x, sign * y) for (x, y) in pts]

for s in (1, -1):
    cut = cq.Workplane("XY").workplane(offset=-1).polyline(cavity_sketch(s)).close().extrude(Z_TOP + 2)
    part = part.cut(cut)

# retention ear slots, open to the bottom
for s in (1, -1):
    for sx in (1, -1):
        for (ya, yb) in ((CAV_Y0 - EAR_D, CAV_Y0 + 0.5), (CAV_Y1 - 0.5, CAV_Y1 + EAR_D)):
            ear = (cq.Workplane("XY").box(CAV_X - EAR_X0, yb - ya, EAR_Z + 1.0, centered=False)
                   .translate((EAR_X0 if sx > 0 else -CAV_X, ya if s > 0 else -yb, -1.0)))
            part = part.cut(ear)

# chamfer cavity rims on the top face
part = part.faces(">Z").edges(cq.selectors.BoxSelector((-CAV_X - 0.5, -CAV_TY - 0.5, Z_TOP - 0.1),
                                                       (CAV_X + 0.5, CAV_TY + 0.5, Z_TOP + 0.1))).chamfer(CAV_CH)

# ---------------- side windows ----------------
for sx in (1, -1):
    for sy in (1, -1):
        # face outward normal angle
        nang = math.degrees(math.atan2(sy * math.sin(math.radians(60)), sx * math.cos(math.radians(60))))
        cx = sx * WIN_CX
        cy = sy * (A_BS - 0.5 * WIN_CX) / math.cos(math.radians(30))
        win = (cq.Workplane("XZ").moveTo(-WIN_W / 2, WIN_Z0).lineTo(WIN_W / 2, WIN_Z0)
               .lineTo(WIN_W / 2, WIN_Z1 - WIN_W / 2)
               .threePointArc((0, WIN_Z1), (-WIN_W / 2, WIN_Z1 - WIN_W / 2)).close()
               .extrude(-(WIN_D + 1.0)).translate((0, -1.0, 0)))
        # local -Y is outward normal; rotate so that -Y -> nang
        win = win.rotate((0, 0, 0), (0, 0, 1), nang + 90).translate((cx, cy, 0))
        part = part.cut(win)

# ---------------- engraved letters ----------------
# single-line stroke letters: centre line offset to a closed outline, flat ends
def stroke_tool(edges, caps, cx, cy):
    w = cq.Wire.assembleEdges(edges)
    o = w.offset2D(LET_W / 2.0, "arc")[0]
    f = cq.Face.makeFromWires(o)
    tool = cq.Workplane().add(cq.Solid.extrudeLinear(f, V(0, 0, LET_D + 1.0)))
    # square off the terminals (remove the round end caps)
    for (px, py, dx, dy) in caps:
        L = LET_W / 2.0 + 0.1
        W = LET_W + 0.2
        bx = (L if dx else W)
        by = (L if dy else W)
        box = (cq.Workplane("XY").box(bx, by, LET_D + 3.0)
               .translate((px + dx * L / 2.0, py + dy * L / 2.0, (LET_D + 1.0) / 2.0)))
        tool = tool.cut(box)
    return tool.translate((cx, cy, Z_TOP - LET_D))

hw, hh = LET_HW, LET_HH
ra = hw
a_s = hh - ra
S_END = 1.64      # |y| of the flat S terminals
G_END = 1.67      # y of the flat upper G terminal
G_BAR_Y = -0.19   # y of the G bar
G_BAR_X = 0.19    # x of the flat inner end of the G bar

# letter S (upper, +Y): two round bowls joined by a straight diagonal spine
S_KNEE = 0.88     # |y| where the spine leaves the sides
S_BEND = 0.9      # radius of the bends at both ends of the spine
s_raw = cq.Wire.assembleEdges([
    cq.Edge.makeLine(V(hw, S_END, 0), V(hw, a_s, 0)),
    cq.Edge.makeThreePointArc(V(hw, a_s, 0), V(0, hh, 0), V(-hw, a_s, 0)),
    cq.Edge.makeLine(V(-hw, a_s, 0), V(-hw, S_KNEE, 0)),
    cq.Edge.makeLine(V(-hw, S_KNEE, 0), V(hw, -S_KNEE, 0)),
    cq.Edge.makeLine(V(hw, -S_KNEE, 0), V(hw, -a_s, 0)),
    cq.Edge.makeThreePointArc(V(hw, -a_s, 0), V(0, -hh, 0), V(-hw, -a_s, 0)),
    cq.Edge.makeLine(V(-hw, -a_s, 0), V(-hw, -S_END, 0)),
])
knees = [v for v in s_raw.Vertices()
         if abs(abs(v.X) - hw) < 1e-6 and abs(abs(v.Y) - S_KNEE) < 1e-6]
s_edges = s_raw.fillet(S_BEND, knees).Edges()
s_caps = [(hw, S_END, 0, -1), (-hw, -S_END, 0, 1)]

# letter G (lower, -Y)
g_edges = [
    cq.Edge.makeLine(V(G_BAR_X, G_BAR_Y, 0), V(hw, G_BAR_Y, 0)),
    cq.Edge.makeLine(V(hw, G_BAR_Y, 0), V(hw, -a_s, 0)),
    cq.Edge.makeThreePointArc(V(hw, -a_s, 0), V(0, -hh, 0), V(-hw, -a_s, 0)),
    cq.Edge.makeLine(V(-hw, -a_s, 0), V(-hw, a_s, 0)),
    cq.Edge.makeThreePointArc(V(-hw, a_s, 0), V(0, hh, 0), V(hw, a_s, 0)),
    cq.Edge.makeLine(V(hw, a_s, 0), V(hw, G_END, 0)),
]
g_caps = [(G_BAR_X, G_BAR_Y, -1, 0), (hw, G_END, 0, -1)]

for edges, caps, cy in ((s_edges, s_caps, LET_Y), (g_edges, g_caps, -LET_Y)):
    part = part.cut(stroke_tool(edges, caps, LET_X, cy))

# ---------------- bottom centre hole ----------------
# blind bore with a 90 deg countersink, made as a revolved cutter on the Z axis
r_h, r_c = HOLE_D / 2.0, HOLE_CS / 2.0
hole = (cq.Workplane("XZ")
        .polyline([(0, -1.0), (r_c + 1.0, -1.0), (r_h, r_c - r_h), (r_h, HOLE_DEPTH), (0, HOLE_DEPTH)])
        .close().revolve(360, (0, 0, 0), (0, 1, 0)))
part = part.cut(hole)

result = part.solids()
VIEW = {"azimuth": 45, "elevation": 26}
